import math

import cadquery as cq

# Companion-cube style block, modelled as the same set of bodies the
# reference shows (they overlap, they are not fused into one):
#   * a core cube with a cross groove cut into every face,
#   * eight corner blocks (cubes with 45 deg chamfers on their inner edges),
#   * twelve small mid-edge blocks,
#   * six round bosses in the middle of the faces.
# Corner and edge blocks are trimmed by a conical dish around every face
# panel (45 deg on the four side faces, 30 deg on top and bottom).

# ---------------- driving dimensions (mm) ----------------
U = 10.0                    # design module; the cube is 12 modules wide
L = 6.0 * U                 # half size of the overall cube
CORE = 5.0 * U              # half size of the recessed core cube (face panels)
C_IN = 1.5 * U              # inner faces of the corner blocks
C_CH = 1.0 * U              # 45 deg chamfer on the corner-block inner edges
C_BEV = 0.2 * U             # bevel on the three outer corner-block edges
E_HALF = 1.0 * U            # half length of the mid-edge blocks
E_OUT = 5.5 * U             # outer faces of the mid-edge blocks
E_IN = 3.5 * U              # inner faces of the mid-edge blocks
E_BEV = 0.1 * U             # bevel on the outer mid-edge block edges

DISH_R0 = 5.0 * U           # dish radius at the outer cube face
DISH_ANG_SIDE = 45.0        # cone half angle, +-X and +-Y faces
DISH_ANG_TOP = 30.0         # cone half angle, +-Z faces

BOSS_R = 2.0 * U            # central boss radius
BOSS_H = 0.25 * U           # central boss height
BOSS_F = 0.1 * U            # boss top edge round
GROOVE_W = 0.2 * U          # width of the cross grooves
GROOVE_D = 0.5 * U          # depth of the cross grooves
DISH_LOW = CORE - GROOVE_D - 0.05 * U   # the dish cutters reach just below the groove floor

FUSE = False                # True: fuse all bodies into a single solid

VIEW = {"azimuth": 45, "elevation": 26}

FACES = ("+Z", "-Z", "+X", "-X", "+Y", "-Y")


# ---------------- helpers ----------------
def to_face(shape, face):
    """Move a feature modelled on the +Z face onto the given face."""
    if face == "+Z":
        return shape
    if face == "-Z":
        return shape.rotate((0, 0, 0), (1, 0, 0), 180)
    if face == "+X":
        return shape.rotate((0, 0, 0), (0, 1, 0), 90)
    if face == "-X":
        return shape.rotate((0, 0, 0), (0, 1, 0), -90)
    if face == "+Y":
        return shape.rotate((0, 0, 0), (1, 0, 0), -90)
    return shape.rotate((0, 0, 0), (1, 0, 0), 90)       # -Y


def dish_cone(face, z_lo, z_hi):
    """Conical cutter on a face: radius DISH_R0 at the outer face,
    shrinking by tan(angle) per mm of depth."""
    ang = DISH_ANG_TOP if face in ("+Z", "-Z") else DISH_ANG_SIDE
    k = math.tan(math.radians(ang))
    r_lo = DISH_R0 - k * (L - z_lo)
    r_hi = DISH_R0 + k * (z_hi - L)
    cone = cq.Solid.makeCone(r_lo, r_hi, z_hi - z_lo,
                             cq.Vector(0, 0, z_lo), cq.Vector(0, 0, 1))
    return to_face(cq.Workplane("XY").add(cone), face)


def on(v, t, tol=1e-3):
    return abs(v - t) < tol


# ---------------- corner blocks ----------------
def corner_block(skip_edge=None):
    """Corner block in the (+,+,+) octant.  skip_edge=(axis, axis) leaves
    the chamfer off the edge lying on the outer face of the first axis and
    the inner face of the second (the reference has one such edge)."""
    s = L - C_IN
    blk = cq.Workplane("XY").box(s, s, s).translate(((L + C_IN) / 2,) * 3).val()
    inner = []
    for e in blk.Edges():
        c = e.Center()
        vals = {"x": c.x, "y": c.y, "z": c.z}
        outer_ax = [a for a, v in vals.items() if on(v, L)]
        inner_ax = [a for a, v in vals.items() if on(v, C_IN)]
        if len(outer_ax) == 1 and len(inner_ax) == 1:   # outer-to-inner face edge
            if skip_edge == (outer_ax[0], inner_ax[0]):
                continue
            inner.append(e)
    blk = blk.chamfer(C_CH, None, inner)
    outer = [e for e in blk.Edges()
             if sum(on(v, L) for v in (e.Center().x, e.Center().y, e.Center().z)) == 2]
    blk = blk.chamfer(C_BEV, None, outer)             # bevel the outer corner edges
    return cq.Workplane("XY").add(blk)


cblk_std = corner_block()
cblk_odd = corner_block(skip_edge=("x", "y"))
corners = []
for sx in (1, -1):
    for sy in (1, -1):
        for sz in (1, -1):
            # the (-X,+Y,-Z) block has no chamfer where its -X face meets
            # its inner +Y-side face
            b = cblk_odd if (sx, sy, sz) == (-1, 1, -1) else cblk_std
            if sx < 0:
                b = b.mirror("YZ")
            if sy < 0:
                b = b.mirror("XZ")
            if sz < 0:
                b = b.mirror("XY")
            corners.append(b)

# ---------------- mid-edge block (along X at +Y,+Z) ----------------
t = E_OUT - E_IN
eblk = (
    cq.Workplane("XY")
    .box(2 * E_HALF, t, t)
    .translate((0, (E_OUT + E_IN) / 2, (E_OUT + E_IN) / 2))
    .val()
)
sel = [e for e in eblk.Edges() if on(e.Center().y, E_OUT) or on(e.Center().z, E_OUT)]
eblk = eblk.chamfer(E_BEV, None, sel)
e0 = cq.Workplane("XY").add(eblk)
x_edges = []
for sy in (1, -1):
    for sz in (1, -1):
        b = e0
        if sy < 0:
            b = b.mirror("XZ")
        if sz < 0:
            b = b.mirror("XY")
        x_edges.append(b)
edge_blocks = list(x_edges)
edge_blocks += [b.rotate((0, 0, 0), (0, 0, 1), 90) for b in x_edges]   # along Y
edge_blocks += [b.rotate((0, 0, 0), (0, 1, 0), 90) for b in x_edges]   # along Z

# ---------------- conical dish around every face panel ----------------
dishes = [dish_cone(f, DISH_LOW, L + U) for f in FACES]


def dish_cut(wp):
    for d in dishes:
        wp = wp.cut(d)
    return wp


# ---------------- core cube with cross grooves ----------------
core = cq.Workplane("XY").box(2 * CORE, 2 * CORE, 2 * CORE)
cross = (
    cq.Workplane("XY")
    .box(2 * L, GROOVE_W, 2 * GROOVE_D)
    .union(cq.Workplane("XY").box(GROOVE_W, 2 * L, 2 * GROOVE_D))
    .translate((0, 0, CORE))
)
for f in FACES:
    core = core.cut(to_face(cross, f))

# ---------------- central bosses with a rounded top edge ----------------
zt = CORE + BOSS_H
zb = CORE - 0.1 * U         # the boss body is sunk slightly into the core
c45 = math.sqrt(0.5)
boss = (
    cq.Workplane("XZ")
    .moveTo(0, zb)
    .lineTo(BOSS_R, zb)
    .lineTo(BOSS_R, zt - BOSS_F)
    .threePointArc(
        (BOSS_R - BOSS_F + c45 * BOSS_F, zt - BOSS_F + c45 * BOSS_F),
        (BOSS_R - BOSS_F, zt),
    )
    .lineTo(0, zt)
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
)
bosses = [to_face(boss, f) for f in FACES]

# ---------------- assemble ----------------
if FUSE:
    blocks = None
    for b in corners + edge_blocks:
        blocks = b if blocks is None else blocks.union(b)
    body = core.union(dish_cut(blocks))
    for b in bosses:
        body = body.union(b)
    result = body
else:
    bodies = [core] + [dish_cut(b) for b in corners + edge_blocks] + bosses
    parts = [s for b in bodies for s in b.val().Solids()]
    result = cq.Workplane("XY").add(cq.Compound.makeCompound(parts))
